import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L_X = 76.0          # box width  (X)
L_Y = 105.0         # box depth  (Y)
H = 30.0            # overall height (Z)
R_CORNER = 3.0      # plan-view corner radius
LID_H = 7.35        # height of the lid band (from the top)
SPLIT_CH = 0.4      # chamfer on the base rim at the parting line

WALL = 2.9          # side wall thickness
TOP_T = 2.9         # lid top thickness
FLOOR_T = 3.1       # floor thickness

# top openings (square, through the lid)
HOLE_X = -15.85
BIG_SQ = 14.2
BIG_Y = 11.85
SMALL_SQ = 8.3
SMALL_Y = -11.85
HOLE_R = 0.3

# side openings on +X wall
CON1_Y = (-44.4, -31.5)
CON1_Z = (1.85, 17.4)
CON2_Y = (-27.7, -17.95)
CON2_Z = (3.9, 11.1)
CON_R = 0.3

# bottom vent/slot
BOT_X = 29.5
BOT_Y = -0.9
BOT_W = 4.7
BOT_L = 8.0

# interior fence and bosses
FENCE_TOP = 6.74
FENCE_T = 1.4
FENCE_Y = -9.25
FENCE_X = 5.0
BOSS_R_TOP = 1.25
BOSS_R_BOT = 1.75
BOSS_HOLE_R = 0.7
BOSS_HOLE_D = 1.2
BOSSES = [(31.55, -16.9, 4.85), (31.55, -42.8, 4.6)]

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- outer body ----------------
# base (lower part) with a small chamfer on its top outer edge, lid band on top:
# together they form the V-shaped parting line around the box
z_split = H - LID_H
base_blk = (
    cq.Workplane("XY")
    .rect(L_X, L_Y)
    .extrude(z_split)
    .edges("|Z").fillet(R_CORNER)
    .faces(">Z").edges().chamfer(SPLIT_CH)
)
lid_blk = (
    cq.Workplane("XY").workplane(offset=z_split)
    .rect(L_X, L_Y)
    .extrude(LID_H)
    .edges("|Z").fillet(R_CORNER)
)
body = base_blk.union(lid_blk)

# ---------------- hollow interior ----------------
cavity = (
    cq.Workplane("XY").workplane(offset=FLOOR_T)
    .rect(L_X - 2 * WALL, L_Y - 2 * WALL)
    .extrude(H - TOP_T - FLOOR_T)
    .edges("|Z").fillet(max(R_CORNER - WALL, 0.3))
)
body = body.cut(cavity)

# ---------------- top openings ----------------
for sq, yc in ((BIG_SQ, BIG_Y), (SMALL_SQ, SMALL_Y)):
    cutter = (
        cq.Workplane("XY").workplane(offset=H - TOP_T - 1)
        .center(HOLE_X, yc)
        .rect(sq, sq)
        .extrude(TOP_T + 2)
        .edges("|Z").fillet(HOLE_R)
    )
    body = body.cut(cutter)

# ---------------- side openings (+X wall) ----------------
for (y0, y1), (z0, z1) in ((CON1_Y, CON1_Z), (CON2_Y, CON2_Z)):
    w = y1 - y0
    h = z1 - z0
    cutter = (
        cq.Workplane("YZ").workplane(offset=L_X / 2 - WALL - 0.01)
        .center((y0 + y1) / 2, (z0 + z1) / 2)
        .rect(w, h)
        .extrude(WALL + 1)
        .edges("|X").fillet(CON_R)
    )
    body = body.cut(cutter)

# ---------------- bottom slot ----------------
bot = (
    cq.Workplane("XY").workplane(offset=-1)
    .center(BOT_X, BOT_Y)
    .rect(BOT_W, BOT_L)
    .extrude(FLOOR_T + 2)
)
body = body.cut(bot)

# ---------------- interior details ----------------
# low fence (battery / board bay) in the -X,-Y quarter
fence_top = FENCE_TOP
fy = FENCE_Y
fx = FENCE_X
inner_x0 = -L_X / 2 + WALL - 0.5   # run 0.5 mm into the walls for a clean fuse
inner_y0 = -L_Y / 2 + WALL - 0.5
fence_a = (
    cq.Workplane("XY").workplane(offset=FLOOR_T - 0.01)
    .center((inner_x0 + fx + FENCE_T / 2) / 2, fy)
    .rect(fx + FENCE_T / 2 - inner_x0, FENCE_T)
    .extrude(fence_top - FLOOR_T + 0.01)
)
fence_b = (
    cq.Workplane("XY").workplane(offset=FLOOR_T - 0.01)
    .center(fx, (inner_y0 + fy) / 2)
    .rect(FENCE_T, fy - inner_y0)
    .extrude(fence_top - FLOOR_T + 0.01)
)
body = body.union(fence_a).union(fence_b)

# small hollow tapered bosses near the connector wall
for (bx, by, btop) in BOSSES:
    h_b = btop - FLOOR_T + 0.01
    cone = cq.Solid.makeCone(
        BOSS_R_BOT, BOSS_R_TOP, h_b,
        pnt=cq.Vector(bx, by, FLOOR_T - 0.01), dir=cq.Vector(0, 0, 1),
    )
    body = body.union(cq.Workplane("XY").add(cone))
    hole = (
        cq.Workplane("XY").workplane(offset=btop - BOSS_HOLE_D)
        .center(bx, by)
        .circle(BOSS_HOLE_R)
        .extrude(BOSS_HOLE_D + 1)
    )
    body = body.cut(hole)

result = body
